import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Spindle unit on a round base: spindle axis along Y (nose towards -Y),
# clamping block on the axis near the origin, round base flange underneath.
# ---------------------------------------------------------------------------

# clamping block
BW = 184.0        # width  (X)
BL = 115.0        # length (Y)
Y_BC = -2.4       # block centre along the spindle axis
BZ_TOP = 86.0     # top face height
BZ_BOT = -86.0    # bottom face height
B_TOP_A = 32.0    # run of the top crown rounding along the top face
B_TOP_D = 9.5     # its drop down the side faces
B_V_A = 26.0      # run of the vertical-edge rounding along front/back faces
B_V_D = 14.0      # its setback along the side faces

# pedestal + base flange
PED_D = 114.0
PED_H = 33.5
BASE_D = 229.0
BASE_T = 23.5

# front flange ring
FR_D = 191.0
FR_L = 50.0
FR_HOLE_R = 84.0          # pitch radius of the two front holes
FR_HOLE_ANG = 153.0       # angle (deg, XZ plane from +X towards +Z)
# front housing
FH_D = 150.0
FH_L = 82.0
FH_REC_D = 110.0          # front recess
FH_REC_DEPTH = 5.0
FH_SCREW_R = 46.5
# spindle nose (radius, y) stations
NECK_R = 20.0
NUT_R = 29.0              # collet nut main body
NUT_SIDE_R = 25.0         # collet nut front / rear shoulders
CONE_R0 = 15.0
CONE_R1 = 6.8
CONE_BORE_R = 3.0
# coolant bracket under the nose
BR_W = 36.0
BR_TOP = -22.0
BR_X = -2.5               # slight offset of the bracket towards -X
# coolant fitting
FIT_ANG = 215.0           # direction in the XZ plane
FIT_Y = -172.0
FIT_REACH = 137.0         # radius of the elbow centre
# rear housing
RH_D = 139.0
RH_L = 181.0
RH_BOLT_R = 60.0
RH_NBOLT = 12
RH_GROOVES = (63.0, 39.0)  # groove distances from the back face
# motor
MO_D = 100.0
MO_L = 162.0
COLLAR_L = 40.0
WIN_ANGS = (48.0, 168.0, 288.0)

Y_BF = Y_BC - BL / 2.0      # block front face
Y_BB = Y_BC + BL / 2.0      # block back face
Y_FR = Y_BF - FR_L          # front of flange ring
Y_FH = Y_FR - FH_L          # front face of front housing
Y_NECK = Y_FH - 7.0         # front of the neck
Y_NUT0 = Y_NECK - 12.0      # rear shoulder -> main nut
Y_NUT1 = Y_NUT0 - 29.0      # main nut -> front shoulder
Y_CONE = Y_NUT1 - 13.5      # front shoulder -> cone
Y_TIP = Y_CONE - 48.5       # cone tip
Y_RH = Y_BB + RH_L          # back of rear housing
Y_MO = Y_RH + MO_L          # back of motor


def cyl_y(d, y0, y1):
    """Cylinder on the spindle axis (X=0,Z=0) between y0 and y1."""
    lo, hi = min(y0, y1), max(y0, y1)
    return (cq.Workplane("XZ", origin=(0, hi, 0))
            .circle(d / 2.0).extrude(hi - lo))


def ring_groove(d, y, w=2.0, depth=1.0):
    """Annular cutter for a shallow groove on a cylinder of diameter d."""
    outer = cyl_y(d + 10.0, y - w / 2.0, y + w / 2.0)
    inner = cyl_y(d - 2.0 * depth, y - w / 2.0, y + w / 2.0)
    return outer.cut(inner)


def polar_xz(r, deg, y):
    a = math.radians(deg)
    return (r * math.cos(a), y, r * math.sin(a))


def at_angle(shape, deg):
    """Rotate a feature built on the +Z side about the spindle axis so that
    it points to angle deg (XZ plane, from +X towards +Z)."""
    return shape.rotate((0, 0, 0), (0, 1, 0), 90.0 - deg)


# ---------------- block ----------------
hw = BW / 2.0
hl = BL / 2.0


def crown_pts(a, d):
    """Rounding tangent to one face (run a) that meets the adjacent face at
    an angle after a drop d: returns (radius, mid-point offsets)."""
    r = (a * a + d * d) / (2.0 * d)
    ang_end = math.atan2(a, r - d)           # swept angle of the arc
    mx = r * math.sin(ang_end / 2.0)
    my = r - r * math.cos(ang_end / 2.0)
    return r, mx, my


# XZ section: crowned top corners
_, tmx, tmz = crown_pts(B_TOP_A, B_TOP_D)
prof_xz = (cq.Workplane("XZ")
           .moveTo(-hw, BZ_BOT)
           .lineTo(hw, BZ_BOT)
           .lineTo(hw, BZ_TOP - B_TOP_D)
           .threePointArc((hw - B_TOP_A + tmx, BZ_TOP - tmz),
                          (hw - B_TOP_A, BZ_TOP))
           .lineTo(-hw + B_TOP_A, BZ_TOP)
           .threePointArc((-hw + B_TOP_A - tmx, BZ_TOP - tmz),
                          (-hw, BZ_TOP - B_TOP_D))
           .close())
block_a = prof_xz.extrude(hl, both=True)

# XY section: vertical edges rounded, tangent to front/back faces
_, vmx, vmy = crown_pts(B_V_A, B_V_D)
prof_xy = (cq.Workplane("XY", origin=(0, 0, BZ_BOT - 1.0))
           .moveTo(-hw + B_V_A, -hl)
           .lineTo(hw - B_V_A, -hl)
           .threePointArc((hw - B_V_A + vmx, -hl + vmy), (hw, -hl + B_V_D))
           .lineTo(hw, hl - B_V_D)
           .threePointArc((hw - B_V_A + vmx, hl - vmy), (hw - B_V_A, hl))
           .lineTo(-hw + B_V_A, hl)
           .threePointArc((-hw + B_V_A - vmx, hl - vmy), (-hw, hl - B_V_D))
           .lineTo(-hw, -hl + B_V_D)
           .threePointArc((-hw + B_V_A - vmx, -hl + vmy), (-hw + B_V_A, -hl))
           .close())
block_b = prof_xy.extrude(BZ_TOP - BZ_BOT + 2.0)
block = block_a.intersect(block_b)

# ---------------- pedestal + base ----------------
ped = (cq.Workplane("XY", origin=(0, 0, BZ_BOT - PED_H))
       .circle(PED_D / 2.0).extrude(PED_H + 1.0))
base = (cq.Workplane("XY", origin=(0, 0, BZ_BOT - PED_H - BASE_T))
        .circle(BASE_D / 2.0).extrude(BASE_T)
        .faces(">Z").edges().chamfer(1.0))

body = block.union(ped).union(base).translate((0, Y_BC, 0))

# ---------------- front flange ring ----------------
ring = cyl_y(FR_D, Y_BF + 0.5, Y_FR)
ring = ring.faces("<Y").edges().chamfer(1.0)
ring = ring.cut(ring_groove(FR_D, Y_BF - 26.0, 1.6, 0.8))
body = body.union(ring)

# ---------------- front housing ----------------
fh = cyl_y(FH_D, Y_FR + 0.5, Y_FH)
fh = fh.faces("<Y").edges().chamfer(1.0)
# boss for the coolant fitting (lower left)
boss = at_angle(cq.Workplane("XY")
                .box(26.0, 40.0, 30.0, centered=(True, False, False))
                .edges("|Y and >Z").chamfer(2.0)
                .translate((0, Y_FH, 60.0)), FIT_ANG)
fh = fh.union(boss)
# stepped front recess with a raised centre ring
fh = fh.cut(cyl_y(FH_REC_D, Y_FH - 1.0, Y_FH + FH_REC_DEPTH))
fh = fh.union(cyl_y(76.0, Y_FH + FH_REC_DEPTH, Y_FH + 1.5))
fh = fh.cut(cyl_y(60.0, Y_FH - 1.0, Y_FH + 9.0))
body = body.union(fh)

# screw heads in the recess
for k in range(4):
    x, y, z = polar_xz(FH_SCREW_R, 45.0 + 90.0 * k, Y_FH + FH_REC_DEPTH)
    s = (cq.Workplane("XZ", origin=(x, y, z)).circle(4.5).extrude(2.5)
         .faces("<Y").workplane().hole(3.0, 1.5))
    body = body.union(s)

# two small locating holes in the recess floor
for a in (15.0, 194.0):
    x, y, z = polar_xz(47.0, a, Y_FH + FH_REC_DEPTH)
    body = body.cut(cq.Workplane("XZ", origin=(x, y, z))
                    .circle(1.5).extrude(-4.0))

# two curved clamp slots in the front face, two small screws in each
for a0 in (207.0, 298.0):
    ann = (cq.Workplane("XZ", origin=(0, Y_FH + 3.0, 0))
           .circle(66.5).circle(55.5).extrude(4.0))
    sector = (cq.Workplane("XZ", origin=(0, Y_FH + 3.5, 0))
              .moveTo(0, 0)
              .lineTo(90.0 * math.cos(math.radians(a0)),
                      90.0 * math.sin(math.radians(a0)))
              .lineTo(90.0 * math.cos(math.radians(a0 + 14.0)),
                      90.0 * math.sin(math.radians(a0 + 14.0)))
              .lineTo(90.0 * math.cos(math.radians(a0 + 28.0)),
                      90.0 * math.sin(math.radians(a0 + 28.0)))
              .close().extrude(5.0))
    body = body.cut(ann.intersect(sector))
    for da in (7.0, 21.0):
        x, y, z = polar_xz(61.0, a0 + da, Y_FH + 3.0)
        body = body.union(cq.Workplane("XZ", origin=(x, y, z))
                          .circle(3.2).extrude(1.5)
                          .faces("<Y").workplane().hole(2.0, 1.0))

# two holes in the flange ring front face
for a in (FR_HOLE_ANG, FR_HOLE_ANG + 180.0):
    x, y, z = polar_xz(FR_HOLE_R, a, Y_FR)
    h = (cq.Workplane("XZ", origin=(x, y, z)).circle(5.5).extrude(-15.0)
         .faces(">Y").edges().fillet(0.5))
    cb = (cq.Workplane("XZ", origin=(x, y - 1.0, z)).circle(7.5)
          .workplane(offset=-2.5).circle(5.5).loft())
    body = body.cut(h).cut(cb)

# ---------------- spindle nose (one revolved profile) ----------------
g = 0.8   # groove depth on the nut
nose_prof = (cq.Workplane("XY")
             .moveTo(0.0, Y_FH + 9.0)
             .lineTo(NECK_R, Y_FH + 9.0)
             .lineTo(NECK_R, Y_NECK)
             .lineTo(NUT_SIDE_R, Y_NECK)
             .lineTo(NUT_SIDE_R, Y_NUT0)
             .lineTo(NUT_R - 1.0, Y_NUT0)
             .lineTo(NUT_R, Y_NUT0 - 1.0)
             .lineTo(NUT_R, Y_NUT0 - 2.0)
             .lineTo(NUT_R - g, Y_NUT0 - 2.5)
             .lineTo(NUT_R, Y_NUT0 - 3.0)
             .lineTo(NUT_R, Y_NUT1 + 3.0)
             .lineTo(NUT_R - g, Y_NUT1 + 2.5)
             .lineTo(NUT_R, Y_NUT1 + 2.0)
             .lineTo(NUT_R, Y_NUT1 + 1.0)
             .lineTo(NUT_R - 1.0, Y_NUT1)
             .lineTo(NUT_SIDE_R, Y_NUT1)
             .lineTo(NUT_SIDE_R, Y_CONE + 3.0)
             .lineTo(NUT_SIDE_R - 3.0, Y_CONE)
             .lineTo(CONE_R0, Y_CONE)
             .threePointArc((10.0, Y_CONE - 24.5), (CONE_R1, Y_TIP))
             .lineTo(CONE_BORE_R, Y_TIP)
             .lineTo(CONE_BORE_R, Y_TIP + 25.0)
             .lineTo(0.0, Y_TIP + 25.0)
             .close())
nose = nose_prof.revolve(360.0, (0, 0, 0), (0, 1, 0))
body = body.union(nose)

# coolant bracket under the nose: ruled loft from a narrow front face to a
# wider foot on the housing, relieved on top around the collet nut
br_front = [(-BR_W / 2.0, BR_TOP), (BR_W / 2.0, BR_TOP),
            (BR_W / 2.0 + 1.0, -51.0), (-BR_W / 2.0 - 1.0, -51.0)]
br_back = [(-BR_W / 2.0, BR_TOP), (BR_W / 2.0, BR_TOP),
           (BR_W / 2.0 + 8.0, -64.0), (-BR_W / 2.0 - 8.0, -64.0)]
br = (cq.Workplane("XZ", origin=(0, Y_FH + 1.0, 0))
      .polyline(br_back).close()
      .workplane(offset=Y_FH + 1.0 - Y_CONE)
      .polyline(br_front).close()
      .loft(ruled=True))
br = br.translate((BR_X, 0, 0))
br = br.cut(cyl_y(2.0 * NUT_R + 2.0, Y_NUT1 - 0.5, Y_FH + 0.5))
body = body.union(br)

# ---------------- coolant fitting ----------------
fa = math.radians(FIT_ANG)
ux, uz = math.cos(fa), math.sin(fa)


def radial_wp(r0):
    return cq.Workplane(cq.Plane(origin=(r0 * ux, FIT_Y, r0 * uz),
                                 xDir=(0, 1, 0), normal=(ux, 0, uz)))


fit = radial_wp(86.0).circle(7.0).extrude(15.0)                # thread
for k in range(4):                                               # thread lines
    fit = fit.cut(radial_wp(91.0 + 2.2 * k).circle(9.0).circle(6.4)
                  .extrude(0.8))
fit = fit.union(radial_wp(100.0).polygon(6, 22.0).extrude(9.0))  # hex
fit = fit.union(radial_wp(109.0).circle(9.5).extrude(FIT_REACH - 109.0))
ec = (FIT_REACH * ux, FIT_Y, FIT_REACH * uz)
fit = fit.union(cq.Workplane("XY").sphere(9.5).translate(ec))
fit = fit.union(cq.Workplane("XZ", origin=ec).circle(9.5).extrude(-20.0))
fit = fit.union(cq.Workplane("XZ", origin=(ec[0], FIT_Y + 16.0, ec[2]))
                .polygon(6, 22.0).extrude(-10.0))
fit = fit.union(cq.Workplane("XZ", origin=(ec[0], FIT_Y + 26.0, ec[2]))
                .circle(7.0).extrude(-6.0))
body = body.union(fit)

# ---------------- rear housing ----------------
rh = cyl_y(RH_D, Y_BB - 0.5, Y_RH)
rh = rh.faces(">Y").edges().fillet(4.0)
for dy in RH_GROOVES:
    rh = rh.cut(ring_groove(RH_D, Y_RH - dy, 2.0, 1.0))
for k in range(RH_NBOLT):
    x, y, z = polar_xz(RH_BOLT_R, 15.0 + 360.0 / RH_NBOLT * k, Y_RH)
    rh = rh.cut(cq.Workplane("XZ", origin=(x, y + 1.0, z))
                .circle(5.5).extrude(4.0))
    rh = rh.union(cq.Workplane("XZ", origin=(x, y - 3.0, z))
                  .circle(4.5).extrude(2.0)
                  .faces(">Y").workplane().polygon(6, 4.0).cutBlind(-1.5))
# small holes in the housing shell
for a, yy in ((90.0, Y_BB + 61.0), (-32.0, Y_BB + 61.0)):
    x, _, z = polar_xz(RH_D / 2.0 + 1.0, a, 0.0)
    rh = rh.cut(cq.Workplane(cq.Plane(origin=(x, yy, z), xDir=(0, 1, 0),
                                      normal=(-x, 0, -z)))
                .circle(1.5).extrude(5.0))
body = body.union(rh)

# ---------------- motor ----------------
mo = cyl_y(MO_D, Y_RH - 0.5, Y_MO)
mo = mo.faces(">Y").edges().chamfer(1.5)
for yy in (Y_RH + 10.0, Y_RH + COLLAR_L, Y_RH + 57.0, Y_RH + 94.0):
    mo = mo.cut(ring_groove(MO_D, yy, 1.5, 0.8))
# clamp windows in the collar, each with a clamping screw
for a in WIN_ANGS:
    win = at_angle(cq.Workplane("XY").box(36.0, COLLAR_L - 6.0, 24.0)
                   .translate((0, Y_RH + COLLAR_L / 2.0, MO_D / 2.0)), a)
    mo = mo.cut(win)
    scr = at_angle(cq.Workplane("XZ",
                                origin=(0, Y_RH + COLLAR_L / 2.0,
                                        MO_D / 2.0 - 12.0))
                   .rect(12.0, 8.0).extrude(9.0, both=True), a)
    mo = mo.union(scr)
# notches around the end cap rim
for k in range(8):
    n = at_angle(cq.Workplane("XY").box(6.0, 6.0, 6.0)
                 .translate((0, Y_MO - 2.0, MO_D / 2.0)), 22.5 + 45.0 * k)
    mo = mo.cut(n)
# two small holes in the motor shell
for a, yy in ((0.0, Y_RH + 121.0), (90.0, Y_RH + 140.0)):
    x, _, z = polar_xz(MO_D / 2.0 + 1.0, a, 0.0)
    mo = mo.cut(cq.Workplane(cq.Plane(origin=(x, yy, z), xDir=(0, 1, 0),
                                      normal=(-x, 0, -z)))
                .circle(1.5).extrude(5.0))
# three small holes on the end face
for zz in (-23.0, 0.0, 23.0):
    mo = mo.cut(cq.Workplane("XZ", origin=(0, Y_MO + 1.0, zz))
                .circle(3.0).extrude(6.0))
body = body.union(mo)

result = body
